import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
FLANGE_D = 42.0          # flange outer diameter
FLANGE_T = 1.70          # flange thickness at the rim
FLANGE_CONE_DEG = 7.0    # draft of the inner (belt side) flange face
TOTAL_H = 14.3           # overall height (flange to flange)
TIP_D = 37.0             # tooth tip diameter of the toothed hub
N_TEETH = 24             # number of belt grooves
GROOVE_R = 1.65          # radius of the round groove
GROOVE_DEPTH = 1.5       # radial depth of the groove below the tip circle
TIP_FILLET = 0.45        # rounding of the tooth tip corners
GROOVE_PHASE_DEG = -45.0 # angular position of one groove centre
HEX_AF = 12.7            # hex bore, across flats (1/2" hex, through)

VIEW = {"azimuth": 45, "elevation": 26}

Rf = FLANGE_D / 2.0
Ro = TIP_D / 2.0
Rroot = Ro - GROOVE_DEPTH
tan_a = math.tan(math.radians(FLANGE_CONE_DEG))

# ---------------- toothed hub ----------------
hub = cq.Workplane("XY").circle(Ro).extrude(TOTAL_H)

# groove = circular arc (radius GROOVE_R) whose bottom lies GROOVE_DEPTH below the tip circle;
# if the groove is deeper than its radius, straight radial walls continue it up to the tip circle
Rc = Rroot + GROOVE_R                                        # groove-arc centre radius
grooves = (
    cq.Workplane("XY")
    .polarArray(Rc, GROOVE_PHASE_DEG, 360, N_TEETH)
    .circle(GROOVE_R)
    .extrude(TOTAL_H)
)
if Rc < Ro:
    wall_len = Ro + 1.0 - Rc
    grooves = grooves.union(
        cq.Workplane("XY")
        .polarArray(Rc + wall_len / 2.0, GROOVE_PHASE_DEG, 360, N_TEETH)
        .rect(wall_len, 2 * GROOVE_R)
        .extrude(TOTAL_H)
    )
hub = hub.cut(grooves)


def _near_radius(r):
    """edge filter: straight vertical edges lying on the circle of radius r"""
    def f(e):
        p = e.Center()
        return abs(math.hypot(p.x, p.y) - r) < 0.05
    return f


# round the tooth tip corners (they lie on the tip circle)
hub = hub.edges("|Z").filter(_near_radius(Ro)).fillet(TIP_FILLET)

# ---------------- flanges (with conical inner face) ----------------
r_in = Rroot - 0.5
rise = (Rf - r_in) * tan_a
flange = (
    cq.Workplane("XY")
    .circle(Rf)
    .extrude(FLANGE_T + rise)
    .faces(">Z")
    .edges()
    .chamfer(rise, Rf - r_in)
)
# turn the flanges so the seam of their round faces sits at the back (-X side)
flange = flange.rotate((0, 0, 0), (0, 0, 1), 180)
bottom_flange = flange
top_flange = flange.mirror("XY").translate((0, 0, TOTAL_H))

body = hub.union(bottom_flange).union(top_flange)

# ---------------- hex bore ----------------
hex_d = HEX_AF / math.cos(math.radians(30))
hex_cut = (
    cq.Workplane("XY")
    .workplane(offset=-1)
    .transformed(rotate=(0, 0, 30))
    .polygon(6, hex_d)
    .extrude(TOTAL_H + 2)
)
result = body.cut(hex_cut)
